import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Gearbox housing: D-shaped block, open pocket on the front (-Y) face.
# Built in a local frame: x = X (length), y = Z (height), z = T - depth
# (z = T is the open front face, z = 0 the back face), then rotated so that
# the front face looks along -Y.
# ---------------------------------------------------------------------------

L = 153.0          # overall length (X)
H = 100.0          # overall height (Z)
T = 32.0           # overall thickness (Y)
RC = 42.0          # corner radius of the rounded (+X) end
RIM = 5.7          # perimeter wall thickness
D_FLOOR = 26.0     # main pocket depth from the front face

# platform (raised gear plate)
PX, PZ = 76.5, 49.6     # platform circle centre
PR = 42.4               # platform circle radius
PW = 28.2               # half width of the neck that joins the top wall
PF = 15.0               # concave blend radius between neck and circle
P_RECESS = 1.0          # platform top is this far below the front face

# left compartment floors
D_UL = 24.5             # upper-left floor depth
D_LL = 19.0             # lower-left (motor) floor depth
Z_SPLIT = 50.2          # height of the step between the two left floors
X_LEFT = 50.0           # right limit of the left compartment floors

# output bearing ring + spokes in the right compartment
BX, BZ = 105.2, 49.9
RING_RO = 27.9
RING_RI = 23.2
BORE_R = 15.7
BORE_CB_R = 17.5       # bearing seat at the bottom of the ring
BORE_DEPTH_BACK = 6.01 # blind depth of the output bore measured from the back face
D_RING = 18.0           # depth of ring / spoke tops
SPOKE_W = 5.5
RIB_X0, RIB_X1 = 105.5, 110.0
D_RIB = 19.0

# screw bosses around the rim
BOSS_R = 4.1
BOSS_HOLE_R = 1.2
BOSS_PTS = [
    (14.2, 92.0), (53.4, 92.0), (92.3, 92.0), (122.9, 89.6), (144.2, 65.8),
    (144.2, 34.2), (122.9, 10.4), (92.3, 8.0), (53.4, 8.0), (14.2, 8.0),
    (7.9, 33.8), (7.9, 66.4),
]

# square-nut traps: (boss centre, direction towards the inside in degrees)
NUT_D = 5.2        # depth of the trap from the front face
NUT_T = 2.8        # trap thickness (along the screw axis)
NUT_W = 5.6        # trap width
NUT_L = 7.0        # trap length from the screw axis towards the cavity
NUT_TRAPS = [
    ((14.2, 92.0), -90.0), ((122.9, 89.6), -135.0), ((144.2, 65.8), 180.0),
    ((144.2, 34.2), 180.0), ((122.9, 10.4), 135.0), ((14.2, 8.0), 90.0),
    ((7.9, 33.8), 0.0), ((7.9, 66.4), 0.0),
]

# motor opening (lower-left)
MX, MZ = 26.6, 26.4
MOTOR_R = 9.75
MOTOR_SLOT_RAD = 15.7
MOTOR_SQ = 32.0
MOTOR_SQ_D = 6.0       # deepest point of the inclined flange seat
MOTOR_SQ_ROT = 45.0

# back face recesses
BACK_D1 = 0.6
BACK_D2 = 1.2


def z_of(depth):
    """local z for a depth measured from the front face"""
    return T - depth


def outline(wp, x0, y0, x1, y1, r):
    """rectangle with the two +x corners rounded by r"""
    return (wp.moveTo(x0, y0).lineTo(x1 - r, y0)
            .threePointArc((x1 - r + r * math.sin(math.pi / 4), y0 + r - r * math.cos(math.pi / 4)), (x1, y0 + r))
            .lineTo(x1, y1 - r)
            .threePointArc((x1 - r + r * math.sin(math.pi / 4), y1 - r + r * math.cos(math.pi / 4)), (x1 - r, y1))
            .lineTo(x0, y1).close())


def slab(profile_fn, z0, z1):
    wp = cq.Workplane("XY").workplane(offset=z0)
    return profile_fn(wp).extrude(z1 - z0)


def platform_profile(wp, ztop, grow=0.0):
    R = PR + grow
    w = PW + grow
    dx = w + PF
    dz = math.sqrt((R + PF) ** 2 - dx ** 2)
    zf = PZ + dz
    ux, uz = -dx / (R + PF), dz / (R + PF)
    tlx, tlz = PX + R * ux, PZ + R * uz
    trx = PX - R * ux
    fcl = (PX - w - PF, zf)
    fcr = (PX + w + PF, zf)
    a_end = math.atan2(-dz, dx)
    ml = (fcl[0] + PF * math.cos(a_end / 2), fcl[1] + PF * math.sin(a_end / 2))
    mr = (fcr[0] - PF * math.cos(a_end / 2), fcr[1] + PF * math.sin(a_end / 2))
    return (wp.moveTo(PX - w, ztop).lineTo(PX - w, zf)
            .threePointArc(ml, (tlx, tlz))
            .threePointArc((PX, PZ - R), (trx, tlz))
            .threePointArc(mr, (PX + w, zf))
            .lineTo(PX + w, ztop).close())


# ---------------- main body ----------------
body = slab(lambda w: outline(w, 0, 0, L, H, RC), 0, T)

pocket = slab(lambda w: outline(w, RIM, RIM, L - RIM, H - RIM, RC - RIM), z_of(D_FLOOR), T + 1)
body = body.cut(pocket)

inner_clip = slab(lambda w: outline(w, RIM - 0.01, RIM - 0.01, L - RIM + 0.01, H - RIM + 0.01, RC - RIM),
                  0, T)

# left compartment floors
upper_left = slab(lambda w: w.moveTo(RIM - 0.1, Z_SPLIT).lineTo(X_LEFT, Z_SPLIT)
                  .lineTo(X_LEFT, H - RIM + 0.1).lineTo(RIM - 0.1, H - RIM + 0.1).close(),
                  z_of(D_FLOOR) - 0.1, z_of(D_UL))
lower_left = slab(lambda w: w.moveTo(RIM - 0.1, RIM - 0.1).lineTo(X_LEFT, RIM - 0.1)
                  .lineTo(X_LEFT, Z_SPLIT).lineTo(RIM - 0.1, Z_SPLIT).close(),
                  z_of(D_FLOOR) - 0.1, z_of(D_LL))
body = body.union(upper_left).union(lower_left)

# raised gear platform
platform = slab(lambda w: platform_profile(w, H - RIM + 0.5), z_of(D_FLOOR) - 0.1, z_of(P_RECESS))
body = body.union(platform)

# right compartment: bearing ring, spokes and a vertical rib
ring = slab(lambda w: w.center(BX, BZ).circle(RING_RO).circle(RING_RI), z_of(D_FLOOR) - 0.1, z_of(D_RING))
spokes = None
for ang in (-40.0, 0.0, 40.0):
    s = (cq.Workplane("XY").workplane(offset=z_of(D_FLOOR) - 0.1)
         .center(BX, BZ).transformed(rotate=(0, 0, ang))
         .center(RING_RO + 20.0, 0).rect(40.0, SPOKE_W).extrude(D_FLOOR - D_RING + 0.1))
    spokes = s if spokes is None else spokes.union(s)
rib = slab(lambda w: w.moveTo(RIB_X0, RIM - 0.1).lineTo(RIB_X1, RIM - 0.1)
           .lineTo(RIB_X1, H - RIM + 0.1).lineTo(RIB_X0, H - RIM + 0.1).close(),
           z_of(D_FLOOR) - 0.1, z_of(D_RIB))
rib = rib.cut(slab(lambda w: w.center(BX, BZ).circle(RING_RI), 0, T))
right_parts = ring.union(spokes.intersect(inner_clip)).union(rib)
body = body.union(right_parts)

# screw bosses around the rim
bosses = (cq.Workplane("XY").workplane(offset=z_of(D_FLOOR) - 0.1)
          .pushPoints(BOSS_PTS).circle(BOSS_R).extrude(D_FLOOR + 0.1))
bosses = bosses.intersect(slab(lambda w: outline(w, 0, 0, L, H, RC), 0, T))
body = body.union(bosses)
body = body.cut(cq.Workplane("XY").workplane(offset=T - 12.0)
                .pushPoints(BOSS_PTS).circle(BOSS_HOLE_R).extrude(13.0))

# square-nut traps crossing the bosses, opening towards the inside
for (bx, bz), ang in NUT_TRAPS:
    trap = (cq.Workplane("XY").workplane(offset=z_of(NUT_D + NUT_T))
            .center(bx, bz).transformed(rotate=(0, 0, ang))
            .center(NUT_L / 2.0 - 1.0, 0).rect(NUT_L, NUT_W).extrude(NUT_T))
    body = body.cut(trap)

# ---------------- holes through the platform ----------------
# bearing bore of the output shaft
body = body.cut(slab(lambda w: w.center(BX, BZ).circle(BORE_R), -1, BORE_DEPTH_BACK))
body = body.cut(slab(lambda w: w.center(BX, BZ).circle(BORE_CB_R), z_of(D_FLOOR + 2.0), z_of(D_FLOOR) + 0.01))

# central blind bore with a key slot through the floor
body = body.cut(slab(lambda w: w.center(PX, 42.7).circle(8.9), z_of(6.5), T + 1))
body = body.cut(slab(lambda w: w.center(75.0, 38.7).slot2D(9.0, 3.0, 90), -1, T + 1))
body = body.cut(slab(lambda w: w.center(71.0, 48.0).circle(1.0), -1, T + 1))

# four gear-shaft holes
GEAR_PTS = [(52.7, 73.5), (100.6, 73.5), (52.7, 25.5), (100.6, 25.5)]
body = body.cut(slab(lambda w: w.pushPoints(GEAR_PTS).circle(4.05), z_of(5.5), T + 1))
# small pilot pattern at the top of the platform
body = body.cut(slab(lambda w: w.center(76.5, 72.9).circle(3.1), z_of(16.0), T + 1))
body = body.cut(slab(lambda w: w.pushPoints([(72.4, 76.9), (80.6, 76.9), (72.4, 68.9), (80.6, 68.9)])
                     .circle(1.2), z_of(10.0), T + 1))
# four small holes around the central bore
body = body.cut(slab(lambda w: w.pushPoints([(65.4, 53.5), (87.4, 53.5), (65.4, 31.4), (87.4, 31.4)])
                     .circle(1.1), z_of(10.0), T + 1))

# ---------------- left compartment ----------------
body = body.cut(slab(lambda w: w.center(MX, MZ).circle(MOTOR_R), -1, T + 1))
motor_slots = [(MX + MOTOR_SLOT_RAD * math.cos(math.radians(a)),
                MZ + MOTOR_SLOT_RAD * math.sin(math.radians(a))) for a in (90, 180, 270, 0)]
for (sx, sz) in motor_slots:
    body = body.cut(slab(lambda w, sx=sx, sz=sz: w.center(sx, sz).slot2D(4.5, 2.0, 45), -1, z_of(D_LL) + 0.01))
body = body.cut(slab(lambda w: w.pushPoints([(14.2, 55.7), (22.7, 55.7)]).circle(1.2), -1, T + 1))

# side holes through the -X wall (2 columns x 3 rows)
side_pts = [(z_of(d), zz) for d in (5.7, 15.4) for zz in (14.0, 49.4, 85.0)]
side = (cq.Workplane("YZ").workplane(offset=-1.0)
        .pushPoints([(zz, zl) for (zl, zz) in side_pts]).circle(1.2).extrude(RIM + 2.0))
body = body.cut(side)

# ---------------- back face ----------------
back_recess = slab(lambda w: platform_profile(w, 92.5, grow=0.5), -1, BACK_D1)
body = body.cut(back_recess)
back_recess2 = slab(lambda w: platform_profile(w, 87.0, grow=-5.0), -1, BACK_D2)
body = body.cut(back_recess2)
body = body.cut(slab(lambda w: w.pushPoints(GEAR_PTS).circle(7.3), -1, 1.8))
body = body.cut(slab(lambda w: w.pushPoints(GEAR_PTS).circle(5.6), -1, 4.0))
body = body.cut(slab(lambda w: w.pushPoints([(75.5, 61.5), (75.5, 37.0)]).slot2D(9.6, 3.0, 90), -1, 3.0))
body = body.cut(slab(lambda w: w.center(50.7, 50.6).circle(7.4), -1, 4.0))
body = body.cut(slab(lambda w: w.center(50.7, 50.6).circle(3.0), -1, 8.0))
body = body.cut(slab(lambda w: w.pushPoints([(65.8, 51.2), (64.3, 19.6)]).circle(1.0), -1, 6.0))

# motor flange seat: square pocket rotated 45 deg with an inclined floor
# (zero depth along its upper-left side, MOTOR_SQ_D deep along the lower-right side)
u_dir = (math.cos(math.radians(-MOTOR_SQ_ROT)), math.sin(math.radians(-MOTOR_SQ_ROT)), 0.0)
n_dir = (u_dir[1], -u_dir[0], 0.0)          # u x z, so the sketch's local y is the depth axis
sq_plane = cq.Plane(origin=(MX, MZ, 0.0), xDir=u_dir, normal=n_dir)
h = MOTOR_SQ / 2.0
wedge = (cq.Workplane(sq_plane)
         .polyline([(-h, -1.0), (h, -1.0), (h, MOTOR_SQ_D), (-h, 0.0)]).close()
         .extrude(h, both=True))
body = body.cut(wedge)

# ---------------- orient: front face looks along -Y, height along +Z ----------------
result = body.rotate((0, 0, 0), (1, 0, 0), 90)
